import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 60.0                 # flange outer radius
H_FLANGE = 14.25         # flange thickness (= pocket floor level)
H_TOTAL = 34.25          # overall height
TOP_FLAT_R = 46.6        # radius where the flat top face ends
CREASE_R = 49.4          # radius of the crease between cone and edge round
CREASE_DROP = 1.35       # height of the edge round band below the top face

TOP_RECESS_R = 33.5      # shallow circular recess in the top face
TOP_RECESS_D = 3.4

BOT_RECESS_R = 42.75     # large circular recess from below
BOT_RECESS_D = 22.5

CENTER_HOLE_D = 13.6
SMALL_HOLE_D = 4.5
SMALL_HOLE_PCD_R = 20.6
N_SMALL = 4

N_POCKETS = 8
POCKET_INNER = 43.5      # distance of pocket back wall from the axis
POCKET_HALF_W = 8.8      # half width of pocket at back wall (sharp corners)
POCKET_FLARE = 33.0      # side-wall angle relative to pocket centre line (deg)
POCKET_CORNER_R = 5.0    # vertical corner fillet inside the pocket

POCKET_HOLE_D = 7.5      # through holes in the pocket floors
POCKET_HOLE_R = 52.2     # radial position of those holes

SEAM_ANG = 45.0          # where periodic-surface seams are parked (deg)

VIEW = {"azimuth": 45, "elevation": 26}

Z = cq.Vector(0, 0, 1)
O = cq.Vector(0, 0, 0)


def zcyl(r, h, x=0.0, y=0.0, z0=0.0, seam=SEAM_ANG):
    """Vertical cylinder (solid) with its seam turned to angle `seam`."""
    c = cq.Solid.makeCylinder(r, h, O, Z).rotate(O, Z, seam)
    return c.translate(cq.Vector(x, y, z0))


# ---------------- main body: revolved flange + cone + rounded top edge -------
# The edge round is tangent to the top face and meets the cone with a crease.
w_band = CREASE_R - TOP_FLAT_R
round_r = (w_band ** 2 + CREASE_DROP ** 2) / (2.0 * CREASE_DROP)
phi = math.asin(w_band / round_r)                    # arc span from the top
zc = H_TOTAL - round_r                               # z of the round's centre
cr, cz = CREASE_R, H_TOTAL - CREASE_DROP
mr = TOP_FLAT_R + round_r * math.sin(phi / 2)
mz = zc + round_r * math.cos(phi / 2)
cone_ang = math.degrees(math.atan2(R - CREASE_R, cz - H_FLANGE))

profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R, 0)
    .lineTo(R, H_FLANGE)
    .lineTo(cr, cz)
    .threePointArc((mr, mz), (TOP_FLAT_R, H_TOTAL))
    .lineTo(0, H_TOTAL)
    .close()
)
body = profile.revolve(360, (0, 0, 0), (0, 1, 0))
# park the seam of the revolved surfaces inside the 135 deg pocket
body = body.rotate((0, 0, 0), (0, 0, 1), 135.0)

# ---------------- top recess ----------------
body = body.cut(zcyl(TOP_RECESS_R, TOP_RECESS_D + 1, z0=H_TOTAL - TOP_RECESS_D))

# ---------------- bottom recess ----------------
body = body.cut(zcyl(BOT_RECESS_R, BOT_RECESS_D + 1, z0=-1, seam=-45.0))

# ---------------- central and small holes ----------------
body = body.cut(zcyl(CENTER_HOLE_D / 2, H_TOTAL + 2, z0=-1))
for i in range(N_SMALL):
    a = math.radians(360.0 / N_SMALL * i)
    body = body.cut(
        zcyl(SMALL_HOLE_D / 2, H_TOTAL + 2,
             SMALL_HOLE_PCD_R * math.cos(a), SMALL_HOLE_PCD_R * math.sin(a), -1)
    )

# ---------------- pockets ----------------
t = math.tan(math.radians(POCKET_FLARE))
d_out = R + 15.0
w_out = POCKET_HALF_W + (d_out - POCKET_INNER) * t
pocket_pts = [
    (POCKET_INNER, -POCKET_HALF_W),
    (d_out, -w_out),
    (d_out, w_out),
    (POCKET_INNER, POCKET_HALF_W),
]
pocket = (
    cq.Workplane("XY")
    .workplane(offset=H_FLANGE)
    .polyline(pocket_pts)
    .close()
    .extrude(H_TOTAL - H_FLANGE + 5)
    .edges("|Z")
    .fillet(POCKET_CORNER_R)
)

for i in range(N_POCKETS):
    ang = 360.0 / N_POCKETS * i
    body = body.cut(pocket.rotate((0, 0, 0), (0, 0, 1), ang))

# ---------------- through holes in the pocket floors ----------------
for i in range(N_POCKETS):
    a = math.radians(360.0 / N_POCKETS * i)
    body = body.cut(
        zcyl(POCKET_HOLE_D / 2, H_FLANGE + 2,
             POCKET_HOLE_R * math.cos(a), POCKET_HOLE_R * math.sin(a), -1)
    )

result = body
